import math
import cadquery as cq

# ---------------------------------------------------------------------------
# Driving dimensions
# ---------------------------------------------------------------------------
DIAMETER = 50.0            # sphere diameter, mm
RADIUS = DIAMETER / 2.0

# Cosmetic only: a B-rep sphere has one seam meridian that shows up as a
# tessellation line in renders.  Its pole axis and seam direction are chosen
# so the seam sits on silhouettes / hidden sides of the standard views.
POLE_AXIS = (1.0, 1.0, 0.0)      # sphere's revolution axis
SEAM_DIR = (-1.0, 1.0, -0.3)     # direction (from centre) of the seam meridian


def _unit(v):
    n = math.sqrt(sum(c * c for c in v))
    return tuple(c / n for c in v)


def _cross(a, b):
    return (a[1] * b[2] - a[2] * b[1], a[2] * b[0] - a[0] * b[2], a[0] * b[1] - a[1] * b[0])


pole = _unit(POLE_AXIS)
seam = SEAM_DIR
dot = sum(a * b for a, b in zip(seam, pole))
seam = _unit(tuple(s - dot * p for s, p in zip(seam, pole)))   # make seam direction perpendicular to pole
normal = _cross(seam, pole)                                     # profile plane: local x = seam, local y = pole

plane = cq.Plane(origin=(0, 0, 0), xDir=seam, normal=normal)

# ---------------------------------------------------------------------------
# Solid sphere: revolve a half-disc profile about the pole axis (local Y).
# ---------------------------------------------------------------------------
result = (
    cq.Workplane(plane)
    .moveTo(0, -RADIUS)
    .threePointArc((RADIUS, 0), (0, RADIUS))
    .close()
    .revolve(360.0, (0, 0, 0), (0, 1, 0))
)

VIEW = {"azimuth": 45, "elevation": 26}
